import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
T = 9.0            # band height (Z)
T_STRIP = 4.5      # height of the perforated strap end
STEP_Y = 12.7      # Y where the strap steps down
HOLE_D = 10.6      # strap holes
SLOT_RIB = 4.2     # rib between the slot and the inner edge of the band
SLOT_R_OUT = 2.0   # corner rounds at the square end of the slot
SLOT_R_IN = 1.0
SLOT_IN_TOP = (-93.0, -10.2)   # inner corner of the square end of the slot
SLOT_IN_END = (-63.4, -48.6)   # inner side runs into the round end here
# outer side of the slot, from the outer corner of the square end round the bottom
SLOT_OUTER = [(-103.0, -12.4), (-100.3, -20.0), (-95.4, -31.0), (-88.0, -40.3),
              (-80.7, -47.9), (-74.6, -53.6), (-70.0, -55.4), (-66.0, -55.0),
              (-63.3, -52.6)]
PEG_D = 8.6        # button pegs
PEG_L = 6.3        # peg protrusion
PEG_DOME = 0.8     # height of the domed head
PEG_RIM = 1.6      # round on the rim of the head
NECK_D = 5.0       # peg neck (the visor sits here)
NECK_L = 1.9
FLEX_W = 1.3       # width of the thin flexible tongue
HOLES = [(-105.5, 59.8), (-106.5, 41.0), (-105.6, 22.3)]   # strap hole centres
PEGS = [((-112.6, -9.0), (-0.99, -0.12)),   # (position on the outer wall, axis)
        ((-34.0, -62.8), (-0.05, -1.0))]
INSERT_L = 21.0    # flush lap-joint insert under the right piece: length
INSERT_H = 4.5     #   and height
PIN_D = 5.0        # pin heads in the joint insert
PIN_POS = (5.0, 15.0)
PIN_DEPTH = 0.8

# ---------------- plan outline (XY) ----------------
# The band is a left piece (strap, slot, narrow front) and a right piece (wider
# section ending in a thin flexible tongue) meeting at a stepped lap joint.
JOINT_IN = (18.5, -54.5)
JOINT_OUT = (20.5, -64.5)

# outer edge of the left piece, from the strap top down round the corner to the joint
OUTER_L = [(-116.2, 69.4), (-117.3, 41.0), (-116.0, 12.7), (-113.4, -5.4),
           (-110.0, -19.3), (-106.1, -31.6), (-102.3, -40.8), (-96.9, -47.8),
           (-89.2, -53.9), (-80.0, -57.8), (-64.6, -60.1), (-49.2, -61.6),
           (-33.7, -62.8), (-20.0, -63.3), (-4.2, -62.3), (13.5, -59.7)]
# inner edge of the left piece, from the joint back up to the strap top
INNER_L = [JOINT_IN, (11.3, -55.8), (-4.2, -58.5), (-20.0, -58.9), (-33.7, -57.8),
           (-41.4, -55.8), (-49.2, -52.8), (-56.9, -48.1), (-64.6, -42.0),
           (-72.3, -34.3), (-80.7, -24.7), (-86.8, -15.4), (-90.7, -5.4),
           (-93.8, 10.0), (-95.6, 41.0), (-93.8, 69.4)]


def offset_pts(pts, d):
    """offset a chain of points sideways (to the right of travel) by d"""
    out = []
    n = len(pts)
    for i, (x, y) in enumerate(pts):
        a = pts[max(i - 1, 0)]
        b = pts[min(i + 1, n - 1)]
        tx, ty = b[0] - a[0], b[1] - a[1]
        L = math.hypot(tx, ty)
        tx, ty = tx / L, ty / L
        out.append((x + ty * d, y - tx * d))
    return out


# thin flexible tongue: centre line with a small outward hook at the end
FLEX_C = [(93.4, -24.2), (100.1, -15.1), (105.6, -7.3), (110.1, -0.4),
          (112.8, 5.5), (114.0, 9.4), (115.7, 11.6), (118.4, 11.7)]
FLEX_OUT = offset_pts(FLEX_C, FLEX_W / 2)
FLEX_IN = offset_pts(FLEX_C, -FLEX_W / 2)
_tx, _ty = FLEX_C[-1][0] - FLEX_C[-2][0], FLEX_C[-1][1] - FLEX_C[-2][1]
_tl = math.hypot(_tx, _ty)
FLEX_TIP = (FLEX_C[-1][0] + _tx / _tl * FLEX_W / 2, FLEX_C[-1][1] + _ty / _tl * FLEX_W / 2)

# outer edge of the right piece: wide section, neck, then the tongue
OUTER_R = [JOINT_OUT, (29.6, -63.2), (39.2, -61.25), (48.6, -58.4), (58.5, -55.0),
           (68.6, -50.6), (79.2, -45.6), (84.5, -42.0), (87.2, -38.8),
           (88.2, -35.0), (88.6, -31.0), (90.4, -27.3)] + FLEX_OUT
# inner edge of the right piece from the tongue tip to the joint
INNER_R = FLEX_IN[::-1] + [(86.9, -27.8), (79.2, -32.6), (68.6, -37.4),
                           (58.5, -41.5), (48.8, -45.4), (39.2, -48.75),
                           (29.6, -51.6), JOINT_IN]

# inner edge of the whole band, from the tongue tip back to the strap top
INNER = INNER_R + INNER_L[1:]

band = (
    cq.Workplane("XY")
    .moveTo(*OUTER_L[0])
    .spline(OUTER_L[1:], includeCurrent=True)
    .threePointArc((17.4, -61.3), JOINT_OUT)      # concave round at the joint step
    .spline(OUTER_R[1:], includeCurrent=True)
    .threePointArc(FLEX_TIP, FLEX_IN[-1])         # rounded end of the tongue
    .spline(INNER[1:], includeCurrent=True)
    .close()
    .extrude(T)
)

# ---------------- perforated strap: thinner, with three holes ----------------
band = band.cut(
    cq.Workplane("XY").box(60, 80, T, centered=(True, False, False))
    .translate((-105, STEP_Y, T_STRIP))
)
band = band.cut(
    cq.Workplane("XY").pushPoints(HOLES).circle(HOLE_D / 2).extrude(T + 2)
    .translate((0, 0, -1))
)

# ---------------- curved slot in the corner (square top end, round bottom end) ----------------
# The slot runs parallel to the inner edge of the band, leaving a rib of SLOT_RIB.
inner_edge = cq.Edge.makeSpline([cq.Vector(x, y, 0) for (x, y) in INNER])


def inner_frame(u):
    """point on the inner edge and the unit normal pointing away from the head"""
    p = inner_edge.positionAt(u)
    t = inner_edge.tangentAt(u)
    L = math.hypot(t.x, t.y)
    return (p.x, p.y), (-t.y / L, t.x / L)


def nearest_u(target, d):
    """parameter whose offset point (distance d) lies closest to target"""
    best, bu = 1e9, 0.0
    for i in range(601):
        u = i / 600.0
        (px, py), (nx, ny) = inner_frame(u)
        dd = (px + d * nx - target[0]) ** 2 + (py + d * ny - target[1]) ** 2
        if dd < best:
            best, bu = dd, u
    return bu


u_end = nearest_u(SLOT_IN_END, SLOT_RIB)   # where the inner side runs into the round end
u_top = nearest_u(SLOT_IN_TOP, SLOT_RIB)   # inner corner of the square end
N_S = 8
us = [u_end + (u_top - u_end) * k / (N_S - 1.0) for k in range(N_S)]
s_in = []
for u in us:
    (px, py), (nx, ny) = inner_frame(u)
    s_in.append((px + SLOT_RIB * nx, py + SLOT_RIB * ny))
slot = (cq.Workplane("XY")
        .moveTo(*s_in[-1])
        .lineTo(*SLOT_OUTER[0])                               # square end
        .spline(SLOT_OUTER[1:] + [s_in[0]], includeCurrent=True)  # outer side and round end
        .spline(s_in[1:], includeCurrent=True)                # inner side, parallel to the band edge
        .close()
        .extrude(T + 2).translate((0, 0, -1)))
band = band.cut(slot)
# rounds in the two corners of the square end
band = band.edges(cq.selectors.NearestToPointSelector(
    (SLOT_OUTER[0][0], SLOT_OUTER[0][1], T / 2))).fillet(SLOT_R_OUT)
band = band.edges(cq.selectors.NearestToPointSelector(
    (s_in[-1][0], s_in[-1][1], T / 2))).fillet(SLOT_R_IN)

# ---------------- button pegs on the outer wall ----------------


def peg(px, py, nx, ny):
    """button peg: short neck and a rounded head, axis along (nx, ny) at mid height"""
    L = math.hypot(nx, ny)
    nx, ny = nx / L, ny / L
    R = PEG_D / 2
    lc = PEG_L - PEG_DOME               # end of the cylindrical part of the head
    rho = (R * R + PEG_DOME * PEG_DOME) / (2 * PEG_DOME)
    a = math.atan2(R, rho - PEG_DOME)   # half angle of the domed cap
    mid = (lc - (rho - PEG_DOME) + rho * math.cos(a / 2), rho * math.sin(a / 2))
    prof = (cq.Workplane("XZ").moveTo(-1.5, 0).lineTo(-1.5, NECK_D / 2)
            .lineTo(NECK_L, NECK_D / 2).lineTo(NECK_L, R).lineTo(lc, R)
            .threePointArc(mid, (PEG_L, 0)).close())
    p = prof.revolve(360, (0, 0, 0), (1, 0, 0))
    p = p.edges(cq.selectors.NearestToPointSelector((lc, 0, 0))).fillet(PEG_RIM)
    p = p.edges(cq.selectors.NearestToPointSelector((NECK_L, 0, 0))).fillet(0.6)
    p = p.rotate((0, 0, 0), (0, 0, 1), math.degrees(math.atan2(ny, nx)))
    return p.translate((px, py, T / 2))


for (ppos, pax) in PEGS:
    band = band.union(peg(ppos[0], ppos[1], pax[0], pax[1]))

# ---------------- lap joint seams ----------------
# The right piece carries a flush rectangular insert of the left piece along its
# underside (tongue with two round pin heads).  The pieces are fused without
# merging faces so the joint seams stay visible as edges.
jx, jy = JOINT_OUT[0] - JOINT_IN[0], JOINT_OUT[1] - JOINT_IN[1]
jdir = math.degrees(math.atan2(jy, jx))          # direction of the joint line
big = 400.0
left_half = (cq.Workplane("XY").rect(big, big, centered=(False, True))
             .extrude(T + 20).translate((0, 0, -10))
             .rotate((0, 0, 0), (0, 0, 1), jdir - 90.0)
             .translate((JOINT_IN[0], JOINT_IN[1], 0)))
JMID = ((JOINT_IN[0] + JOINT_OUT[0]) / 2, (JOINT_IN[1] + JOINT_OUT[1]) / 2)
tang = jdir + 90.0                                 # band direction at the joint
tab_box = (cq.Workplane("XY").rect(INSERT_L, 40, centered=(False, True))
           .extrude(INSERT_H)
           .rotate((0, 0, 0), (0, 0, 1), tang)
           .translate((JMID[0], JMID[1], 0)))
ca, sa = math.cos(math.radians(tang)), math.sin(math.radians(tang))
pin_pts = [(JMID[0] + d * ca, JMID[1] + d * sa) for d in PIN_POS]
band = band.cut(cq.Workplane("XY").pushPoints(pin_pts).circle(PIN_D / 2)
                .extrude(PIN_DEPTH + 1).translate((0, 0, -1)))

piece_ab = band.intersect(left_half.union(tab_box))      # left piece with its tongue
piece_c = band.cut(left_half).cut(tab_box)               # right piece
result = piece_ab.union(piece_c, clean=False)
